import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Stormtrooper-helmet mug.
# Built in a canonical frame (face toward -Y, handle toward +Y, foot on z=0),
# then turned about Z by YAW to match the reference orientation.
# ---------------------------------------------------------------------------
YAW = -24.0          # rotation of the whole mug about Z (deg)

# ---- cup ------------------------------------------------------------------
H = 93.0             # overall height
R_TOP = 44.0         # outer radius of the rim
R_IN_TOP = 38.3      # cavity radius at the rim
R_IN_BOT = 36.5      # cavity radius at the floor
FLOOR_Z = 9.0        # cavity floor height
FLOOR_FILLET = 8.0
RIM_FILLET = 2.0

BASE_R0 = 47.8       # foot radius at the ground
BASE_R1 = 45.5       # foot radius at its top
BASE_H = 6.0
BASE_OFF = -6.0      # foot centre offset toward the face

# helmet shell: lofted elliptic sections (z, half width x, half depth y, centre y)
BODY_SECT = [(4.0, 42.5, 42.5, 0.0), (16.0, 46.5, 45.0, -1.0), (33.0, 56.0, 49.5, -3.0),
             (52.0, 48.5, 47.3, 0.0), (80.0, 46.0, 45.9, 0.0), (H, R_TOP, R_TOP, 0.0)]

# ---- face masses: spheroids ((semi axes), centre) ----------------------------
UPPER_FACE = ((48.0, 48.0, 42.0), (0.0, -9.5, 45.0))   # brow / nose / cheeks
JAW = ((32.0, 32.0, 18.0), (0.0, -31.0, 28.0))         # chin between the lobes
LOBE_A, LOBE_B, LOBE_C = 22.0, 17.0, 17.0              # cheek lobes (long, round)
LOBE_X, LOBE_Y, LOBE_Z = 24.5, -43.2, 27.5
LOBE_ROT = 50.0
LOBE_VENT = (7.5, 6.0, 3.2, 21.0, 76.0)   # oval semi axes, depth, height, angle off front

GRILLE_R = 9.5       # breathing grille (vertical fluted post)
GRILLE_Y = -57.5
GRILLE_Z0, GRILLE_Z1 = 8.0, 43.0
GRILLE_FLUTES = (-6.4, -3.2, 0.0, 3.2, 6.4)

# ---- eyes, tears, frown ------------------------------------------------------
EYE_ANG = -60.0      # direction of the eye centre (deg from +x toward +y)
EYE_PTS = [(-16.0, 80.0), (-5.0, 80.2), (6.0, 79.2), (15.0, 77.0), (19.0, 72.5),
           (16.5, 67.5), (8.0, 66.3), (0.0, 68.0), (-8.0, 72.0), (-13.5, 76.5)]
TEAR_ANG = -40.0
TEAR_PTS = [(-7.5, 67.0), (0.0, 67.0), (9.0, 48.5), (0.5, 48.5)]
EYE_FLOOR = (46.0, 64.0, 42.6, 82.0)   # recess floor cone: (r, z) at bottom and top

FROWN_UP = [(-27.0, 47.5), (0.0, 64.0), (27.0, 47.5)]
FROWN_LO = [(27.0, 43.0), (0.0, 59.5), (-27.0, 43.0)]
FROWN_T = 1.2        # relief of the frown ridge
TEETH = 5            # teeth slots per side

# ---- brow band, temple tabs, ears, back vents ---------------------------------
BAND_T = 2.2              # relief of brow band, temple tabs and ear stems
BAND_TOP = (88.5, 0.25)   # top edge: height at the front (y=-45), drop per mm toward +y
BAND_BOT = (80.0, 0.17)   # bottom edge
BAND_END_Y = 12.0         # band stops behind this y
TAB_PTS = [(-9.5, 73.0), (9.5, 73.0), (6.0, 91.0), (-6.0, 91.0)]
TAB_ANG = -8.0

EAR_Z = 59.5
EAR_R = 11.5
EAR_T = 3.0
STEM_PTS = [(-2.6, EAR_Z - 8.0), (2.6, EAR_Z - 8.0), (4.6, 22.0), (3.0, 16.0),
            (-3.5, 16.0), (-4.2, 22.0)]

VENT_ANG = 58.5      # back vents: angle from +x toward +y (deg)
VENT_Z0, VENT_Z1 = 65.0, 84.0
VENT_WB, VENT_WT = 24.0, 16.0
VENT_D = 1.6

# ---- handle ---------------------------------------------------------------------
HANDLE_W = 13.0      # handle width (perpendicular to its plane)
HANDLE_YC = 42.0     # centre of the D-loop ellipses (distance from the axis)
HANDLE_ZC = 49.5
HANDLE_AO, HANDLE_BO = 29.0, 36.0   # outer half-ellipse semi axes (radial, vertical)
HANDLE_AI, HANDLE_BI = 21.5, 26.5   # inner half-ellipse semi axes


# ---------------------------------------------------------------------------
def ellipsoid(a, b, c, center=(0, 0, 0), rot_z=0.0):
    """Spheroid of revolution.  a == b: axis vertical (radial a, half height c);
    otherwise b == c is assumed: axis along x (half length a, radius b)."""
    if abs(a - b) < 1e-9:
        prof = (cq.Workplane("XZ").moveTo(0, -c)
                .ellipseArc(a, c, -90, 90, sense=1, makeWire=False).close())
        e = prof.revolve(360, (0, 0, 0), (0, 1, 0)).val()
    else:
        prof = (cq.Workplane("XY").moveTo(-a, 0)
                .ellipseArc(a, b, 0, 180, sense=-1, startAtCurrent=True, makeWire=False).close())
        e = prof.revolve(360, (-a, 0, 0), (a, 0, 0)).val()
    if rot_z:
        e = e.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), rot_z)
    return cq.Workplane("XY").add(e.translate(cq.Vector(*center)))


def shell(dr):
    """Lofted helmet shell (elliptic sections, four patches) pushed out by dr."""
    wires = []
    for z, a, b, yc in BODY_SECT:
        edges = [cq.Edge.makeEllipse(a + dr, b + dr, cq.Vector(0, yc, z), cq.Vector(0, 0, 1),
                                     cq.Vector(1, 0, 0), q * 90.0, q * 90.0 + 90.0)
                 for q in range(4)]
        wires.append(cq.Wire.assembleEdges(edges))
    return cq.Workplane("XY").add(cq.Solid.makeLoft(wires, False))


def radial_prism(pts2d, ang_deg, r0=20.0, length=50.0, smooth=False):
    """Outline given as (tangential, z) points, extruded radially outward
    from radius r0 in direction ang_deg (angle from +x toward +y)."""
    wp = cq.Workplane("YZ").workplane(offset=r0)
    wp = wp.spline(pts2d, periodic=True).close() if smooth else wp.polyline(pts2d).close()
    return wp.extrude(length).rotate((0, 0, 0), (0, 0, 1), ang_deg)


def mirror_ang(ang):
    return 180.0 - ang


def batch(parts):
    """Gather the solids of several workplanes into one compound tool."""
    solids = []
    for p in parts:
        solids.extend(p.solids().vals())
    return cq.Workplane("XY").add(cq.Compound.makeCompound(solids))


def half_space(z_front, slope, below):
    """Half space under (below=True) or over a plane tilted about x."""
    tilt = math.degrees(math.atan(slope))
    box = cq.Workplane("XY").box(300, 300, 100).translate((0, 0, -50 if below else 50))
    return box.rotate((0, 0, 0), (1, 0, 0), -tilt).translate((0, 0, z_front - slope * 45.0))


def face_front_y(x, z):
    """y of the upper-face ellipsoid surface (front side) at (x, z)."""
    (a, b, c), (cx, cy, cz) = UPPER_FACE
    k = 1.0 - ((x - cx) / a) ** 2 - ((z - cz) / c) ** 2
    return cy - b * math.sqrt(max(k, 0.0))


# ---------------- helmet shell, rim and foot ----------------------------------
body = shell(0.0)
body = body.faces(">Z").edges().fillet(RIM_FILLET)

foot = (cq.Workplane("XY").center(0, BASE_OFF)
        .circle(BASE_R0).workplane(offset=BASE_H).circle(BASE_R1).loft())

# ---------------- face masses ---------------------------------------------------
masses = [foot] + [ellipsoid(a, b, c, ctr) for (a, b, c), ctr in (UPPER_FACE, JAW)]
va, vb, vd, vz, voff = LOBE_VENT
for sgn in (1, -1):
    lobe = ellipsoid(LOBE_A, LOBE_B, LOBE_C, (0, 0, 0), sgn * LOBE_ROT) \
        .translate((sgn * LOBE_X, LOBE_Y, LOBE_Z))
    core = ellipsoid(LOBE_A - vd, LOBE_B - vd, LOBE_C - vd, (0, 0, 0), sgn * LOBE_ROT) \
        .translate((sgn * LOBE_X, LOBE_Y, LOBE_Z))
    oval = (cq.Workplane("YZ").workplane(offset=56.0).center(0, vz)
            .ellipse(va, vb).extrude(20.0)
            .rotate((0, 0, 0), (0, 0, 1), -90.0 + sgn * (90.0 - voff)))
    masses.append(lobe.cut(oval.cut(core)))
body = body.union(batch(masses), clean=False)

# notch between the lobes for the grille
NOTCH_W = 18.0
notch = (cq.Workplane("XZ", origin=(0, -52.0, 0))
         .moveTo(-NOTCH_W / 2, 8.0).lineTo(NOTCH_W / 2, 8.0)
         .lineTo(NOTCH_W / 2, GRILLE_Z1 - NOTCH_W / 2 - 2.0)
         .threePointArc((0, GRILLE_Z1 - 2.0), (-NOTCH_W / 2, GRILLE_Z1 - NOTCH_W / 2 - 2.0))
         .close().extrude(40.0))
body = body.cut(notch, clean=False)

# ---------------- raised details -------------------------------------------------
adds = []

# fluted breathing grille
grille = (cq.Workplane("XY").workplane(offset=GRILLE_Z0).center(0, GRILLE_Y)
          .circle(GRILLE_R).extrude(GRILLE_Z1 - GRILLE_Z0)
          .faces(">Z").edges().fillet(GRILLE_R - 0.5)
          .faces("<Z").edges().fillet(3.0))
for xg in GRILLE_FLUTES:
    ys = GRILLE_Y - math.sqrt(GRILLE_R ** 2 - xg ** 2)
    grille = grille.cut(cq.Workplane("XY").workplane(offset=10.0)
                        .center(xg, ys - 1.0).rect(1.1, 4.0)
                        .extrude(GRILLE_Z1 - 13.0))
adds.append(grille)

# frown ridge (inverted V under the nose) with its row of teeth
(fa, fb, fc), fctr = UPPER_FACE
frown = radial_prism(FROWN_UP + FROWN_LO, -90.0).intersect(
    ellipsoid(fa + FROWN_T, fb + FROWN_T, fc + FROWN_T, fctr))
slope = (FROWN_UP[1][1] - FROWN_UP[0][1]) / (FROWN_UP[2][0] - FROWN_UP[1][0])
z_mid = 0.5 * (FROWN_UP[1][1] + FROWN_LO[1][1])
teeth = []
for sgn in (1, -1):
    for i in range(TEETH):
        t = 3.5 + i * 4.6
        zc = z_mid - t * slope - 0.2
        y0 = face_front_y(t, zc) + 0.5
        teeth.append(cq.Workplane("XZ", origin=(0, y0, 0)).center(sgn * t, zc)
                     .rect(2.4, 3.2).extrude(10.0)
                     .rotate((sgn * t, 0, zc), (sgn * t, 1, zc),
                             sgn * math.degrees(math.atan(slope))))
adds.append(frown.cut(batch(teeth)))

# brow band (tilted, edges converging toward the back), temple tabs and the
# keyhole stems under the ears: one relief cut from a single offset shell
front = cq.Workplane("XY").box(200, 100, 200).translate((0, BAND_END_Y - 50, 0))
region = (half_space(*BAND_TOP, True).intersect(half_space(*BAND_BOT, False))
          .intersect(front))
for ang in (TAB_ANG, mirror_ang(TAB_ANG)):
    region = region.union(radial_prism(TAB_PTS, ang))
for sgn in (1, -1):
    region = region.union(radial_prism([(sgn * t, z) for t, z in STEM_PTS],
                                       0.0 if sgn > 0 else 180.0))
adds.append(shell(BAND_T).intersect(region))

# ear discs with vent bars
EAR_X = 47.0 + EAR_T          # outer face of the ear disc
for sgn in (1, -1):
    ear = (cq.Workplane("YZ").workplane(offset=sgn * 43.0)
           .center(0, EAR_Z).circle(EAR_R).extrude(sgn * (EAR_X - 43.0))
           .faces(">X" if sgn > 0 else "<X").edges().fillet(2.5))
    for i in range(4):
        ear = ear.union(cq.Workplane("XY").box(2.6, 0.8, 5.0)
                        .translate((sgn * (EAR_X + 0.8), -2.7 + i * 1.8, EAR_Z)))
    adds.append(ear)

# D-shaped handle
outer = (cq.Workplane("YZ").center(HANDLE_YC, HANDLE_ZC)
         .ellipse(HANDLE_AO, HANDLE_BO, rotation_angle=180).extrude(HANDLE_W / 2, both=True))
inner = (cq.Workplane("YZ").center(HANDLE_YC, HANDLE_ZC)
         .ellipse(HANDLE_AI, HANDLE_BI, rotation_angle=180).extrude(HANDLE_W, both=True))
keep = cq.Workplane("XY").center(0, HANDLE_YC + 50).rect(40, 100).extrude(H)
adds.append(outer.cut(inner).intersect(keep))

body = body.union(batch(adds), clean=False)

# ---------------- recessed details ------------------------------------------------
cuts = []

# eye lenses and cheek "tears"
floor_cyl = (cq.Workplane("XY").workplane(offset=EYE_FLOOR[1]).circle(EYE_FLOOR[0])
             .workplane(offset=EYE_FLOOR[3] - EYE_FLOOR[1]).circle(EYE_FLOOR[2]).loft())
floor_cyl = floor_cyl.union(cq.Workplane("XY").circle(EYE_FLOOR[0]).extrude(EYE_FLOOR[1]))
under_band = half_space(*BAND_BOT, True)
for sgn in (1, -1):
    eye = radial_prism([(sgn * t, z) for t, z in EYE_PTS],
                       EYE_ANG if sgn > 0 else mirror_ang(EYE_ANG), smooth=True)
    tear = radial_prism([(sgn * t, z) for t, z in TEAR_PTS],
                        TEAR_ANG if sgn > 0 else mirror_ang(TEAR_ANG))
    cuts.append(eye.union(tear).cut(floor_cyl).intersect(under_band))

# back vents (recessed trapezoids)
vent_pts = [(-VENT_WB / 2, VENT_Z0), (VENT_WB / 2, VENT_Z0),
            (VENT_WT / 2, VENT_Z1), (-VENT_WT / 2, VENT_Z1)]
vent_env = shell(-VENT_D)
for ang in (VENT_ANG, mirror_ang(VENT_ANG)):
    cuts.append(radial_prism(vent_pts, ang).cut(vent_env))

# drinking cavity
cav = (cq.Workplane("XY").workplane(offset=FLOOR_Z)
       .circle(R_IN_BOT).workplane(offset=H + 5 - FLOOR_Z).circle(R_IN_TOP + 0.3).loft())
cav = cav.faces("<Z").edges().fillet(FLOOR_FILLET)
cuts.append(cav.rotate((0, 0, 0), (0, 0, 1), -105.0))   # seam where it is hardly seen

body = body.cut(batch(cuts), clean=False)

result = body.rotate((0, 0, 0), (0, 0, 1), YAW)
